import cadquery as cq
import math

# ---------------------------------------------------------------
# Pan / tilt kit for micro servos: six separate printed parts laid
# out side by side (units: mm).
#   A  tilt platform with ears, back tab and snap legs
#   B  tilt bracket (servo cradle + web + lug with hole)
#   C  tilt bracket, mirrored (servo cradle + web + lug with pin)
#   D  square pan base plate with hollow cup underneath
#   E  single servo horn
#   F  round pulley / disc horn
# ---------------------------------------------------------------

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def xz_prism(pts, y0, y1):
    """polygon given in (x, z), extruded along Y from y0 to y1"""
    pl = cq.Plane(origin=(0, y1, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    return cq.Workplane(pl).polyline(pts).close().extrude(y1 - y0)


def yz_prism(pts, x0, x1):
    """polygon given in (y, z), extruded along X from x0 to x1"""
    pl = cq.Plane(origin=(x0, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    return cq.Workplane(pl).polyline(pts).close().extrude(x1 - x0)


def xz_cyl(cx, cz, r, y0, y1):
    pl = cq.Plane(origin=(cx, y1, cz), xDir=(1, 0, 0), normal=(0, -1, 0))
    return cq.Workplane(pl).circle(r).extrude(y1 - y0)


def yz_cyl(cy, cz, r, x0, x1):
    pl = cq.Plane(origin=(x0, cy, cz), xDir=(0, 1, 0), normal=(1, 0, 0))
    return cq.Workplane(pl).circle(r).extrude(x1 - x0)


def z_cyl(cx, cy, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(cx, cy).circle(r).extrude(z1 - z0))


# =================================================================
# Part D : square pan base plate
# =================================================================
D_X0, D_X1 = 94.7, 155.3
D_Y0, D_Y1 = 116.7, 170.6
D_Z0, D_Z1 = 143.6, 148.1
D_HOLE = (117.8, 143.7)      # centre hole / cup axis (offset toward -X)
D_HOLE_R = 3.8
D_CBORE_R = 4.7
D_CBORE_DEPTH = 1.5
D_CUP_R = 18.9
D_CUP_WALL = 1.5
D_CUP_Z0 = 132.1
D_CORNER_INSET = 5.2
D_CORNER_HOLE_R = 1.35
D_CORNER_CB_R = 2.7
D_CORNER_CB_DEPTH = 2.0
D_POCKET_INSET = 2.2
D_POCKET_DEPTH = 1.0
D_BOSS_R = 5.6


def make_D():
    p = box(D_X0, D_X1, D_Y0, D_Y1, D_Z0, D_Z1).edges("|Z").fillet(1.0)
    # shallow top pocket leaving raised quarter bosses at the corners
    pk = box(D_X0 + D_POCKET_INSET, D_X1 - D_POCKET_INSET,
             D_Y0 + D_POCKET_INSET, D_Y1 - D_POCKET_INSET,
             D_Z1 - D_POCKET_DEPTH, D_Z1 + 1)
    corners = [(D_X0 + D_CORNER_INSET, D_Y0 + D_CORNER_INSET),
               (D_X1 - D_CORNER_INSET, D_Y0 + D_CORNER_INSET),
               (D_X0 + D_CORNER_INSET, D_Y1 - D_CORNER_INSET),
               (D_X1 - D_CORNER_INSET, D_Y1 - D_CORNER_INSET)]
    for (cx, cy) in corners:
        pk = pk.cut(z_cyl(cx, cy, D_BOSS_R, D_Z0, D_Z1 + 2))
    p = p.cut(pk)
    # hollow cup underneath
    cup = z_cyl(D_HOLE[0], D_HOLE[1], D_CUP_R, D_CUP_Z0, D_Z0 + 0.01)
    cup = cup.cut(z_cyl(D_HOLE[0], D_HOLE[1], D_CUP_R - D_CUP_WALL,
                        D_CUP_Z0 - 1, D_Z0))
    p = p.union(cup)
    # holes
    p = p.cut(z_cyl(D_HOLE[0], D_HOLE[1], D_HOLE_R, D_Z0 - 5, D_Z1 + 5))
    p = p.cut(z_cyl(D_HOLE[0], D_HOLE[1], D_CBORE_R,
                    D_Z1 - D_POCKET_DEPTH - D_CBORE_DEPTH, D_Z1 + 5))
    for (cx, cy) in corners:
        p = p.cut(z_cyl(cx, cy, D_CORNER_HOLE_R, D_Z0 - 5, D_Z1 + 5))
        p = p.cut(z_cyl(cx, cy, D_CORNER_CB_R, D_Z0 - 5, D_Z0 + D_CORNER_CB_DEPTH))
    return p


# =================================================================
# Part F : round disc horn / pulley
# =================================================================
F_C = (178.6, 229.2)
F_R = 16.35
F_Z0, F_Z1 = 139.6, 143.4
F_HUB_R = 4.7
F_HUB_Z0 = 136.5
F_HOLE_R = 3.6
F_GROOVE = 0.8


def make_F():
    cx, cy = F_C
    prof = [(0, F_HUB_Z0), (F_HUB_R, F_HUB_Z0), (F_HUB_R, F_Z0),
            (F_R - 0.5, F_Z0), (F_R, F_Z0 + 0.5), (F_R, F_Z1 - 1.25),
            (F_R - F_GROOVE, F_Z1 - 0.9), (F_R, F_Z1 - 0.55),
            (F_R, F_Z1), (0, F_Z1)]
    pl = cq.Plane(origin=(cx, cy, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    d = (cq.Workplane(pl).polyline(prof).close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
    d = d.cut(z_cyl(cx, cy, F_HOLE_R, F_HUB_Z0 - 2, F_Z1 + 2))
    return d


# =================================================================
# Part E : single arm servo horn
# =================================================================
E_HUB = (212.4, 169.1)
E_HUB_R = 4.5
E_BORE_R = 3.5
E_Z0 = 140.6
E_ARM_T = 3.0
E_HUB_TOP = 148.0
E_TIP_X = 235.1
E_ROOT_HALF = 5.2
E_TIP_HALF = 3.5


def make_E():
    hx, hy = E_HUB
    tcx = E_TIP_X - E_TIP_HALF
    pts = [(hx, hy - E_ROOT_HALF), (tcx, hy - E_TIP_HALF),
           (tcx, hy + E_TIP_HALF), (hx, hy + E_ROOT_HALF)]
    arm = (cq.Workplane("XY").workplane(offset=E_Z0)
           .polyline(pts).close().extrude(E_ARM_T))
    arm = arm.union(z_cyl(hx, hy, E_ROOT_HALF, E_Z0, E_Z0 + E_ARM_T))
    arm = arm.union(z_cyl(tcx, hy, E_TIP_HALF, E_Z0, E_Z0 + E_ARM_T))
    arm = arm.union(z_cyl(hx, hy, E_HUB_R, E_Z0, E_HUB_TOP))
    arm = arm.cut(z_cyl(hx, hy, E_BORE_R, E_Z0 - 1, E_HUB_TOP + 1))
    return arm


# =================================================================
# Part A : tilt platform
# =================================================================
A_X0, A_X1 = 11.1, 69.2          # wide front section
A_Y0, A_YS = 35.4, 82.3          # front edge, step to narrow section
A_BX0, A_BX1 = 19.2, 61.5        # narrow back section
A_Y1 = 97.7                      # back edge
A_Z0, A_Z1 = 139.3, 143.0
A_CORNER_R = 12.8
A_NOTCH = (49.9, 56.3, 92.3)     # back edge notch x0, x1, y0 (dovetail)
A_NOTCH_LIP = 0.7
A_SLOT_Y = (52.0, 76.0)
A_SLOT_L = (15.5, 22.2)
A_SLOT_R = (58.6, 65.2)
A_LEG_L = (13.0, 16.5)
A_LEG_R = (63.7, 67.2)
A_LEG_Z0 = 121.0
A_LEG_Y = (52.0, 75.5)
A_EAR_T = 3.0
UB_X0, UB_X1 = 27.9, 52.4        # rib box under the plate
UB_Y0, UB_Y1 = 36.5, 39.7
UB_Z0 = 136.2


def make_A():
    # plate outline
    prof = (cq.Workplane("XY").workplane(offset=A_Z0)
            .polyline([(A_X0, A_Y0), (A_X1, A_Y0), (A_X1, A_YS),
                       (A_BX1, A_YS), (A_BX1, A_Y1),
                       (A_NOTCH[1] - A_NOTCH_LIP, A_Y1),
                       (A_NOTCH[1], A_NOTCH[2]),
                       (A_NOTCH[0], A_NOTCH[2]),
                       (A_NOTCH[0] + A_NOTCH_LIP, A_Y1),
                       (A_BX0, A_Y1), (A_BX0, A_YS), (A_X0, A_YS)])
            .close().extrude(A_Z1 - A_Z0))
    prof = (prof.edges("|Z")
            .edges(cq.selectors.BoxSelector((A_X0 - 1, A_Y0 - 1, A_Z0 - 1),
                                            (A_X1 + 1, A_Y0 + 1, A_Z1 + 1)))
            .fillet(A_CORNER_R))
    a = prof
    # snap legs with small inward hooks
    for (x0, x1), hook in ((A_LEG_L, +1), (A_LEG_R, -1)):
        a = a.union(box(x0, x1, A_LEG_Y[0], A_LEG_Y[1], A_LEG_Z0, A_Z0 + 0.01))
        if hook > 0:
            a = a.union(box(x1, x1 + 1.8, A_LEG_Y[0], A_LEG_Y[1],
                            A_LEG_Z0, A_LEG_Z0 + 1.8))
        else:
            a = a.union(box(x0 - 1.8, x0, A_LEG_Y[0], A_LEG_Y[1],
                            A_LEG_Z0, A_LEG_Z0 + 1.8))
    # slots through the plate beside the legs
    for (x0, x1) in (A_SLOT_L, A_SLOT_R):
        a = a.cut(box(x0, x1, A_SLOT_Y[0], A_SLOT_Y[1], A_Z0 - 1, A_Z1 + 1))

    # small ear at the front centre (YZ plane)
    ex0 = 35.0
    ear_c = (53.2, 153.9)
    ear_r = 3.4
    ear = yz_prism([(40.7, A_Z1 - 0.01), (56.6, A_Z1 - 0.01),
                    (56.6, ear_c[1]), (ear_c[0] - ear_r * 0.85, ear_c[1] + ear_r * 0.5)],
                   ex0, ex0 + A_EAR_T)
    ear = ear.union(yz_cyl(ear_c[0], ear_c[1], ear_r, ex0, ex0 + A_EAR_T))
    ear = ear.cut(yz_cyl(ear_c[0], ear_c[1], 1.5, ex0 - 1, ex0 + A_EAR_T + 1))
    a = a.union(ear)

    # big ear at the right edge (YZ plane)
    bx1 = A_X1 - 0.5
    bx0 = bx1 - A_EAR_T
    big_c = (83.4, 154.4)
    big_r = 6.6
    big = yz_prism([(59.3, A_Z1 - 0.01), (82.4, A_Z1 - 0.01),
                    (big_c[0] + big_r * 0.72, big_c[1] - big_r * 0.69),
                    (big_c[0] - big_r * 0.72, big_c[1] + big_r * 0.69)],
                   bx0, bx1)
    big = big.union(yz_cyl(big_c[0], big_c[1], big_r, bx0, bx1))
    big = big.cut(yz_cyl(big_c[0], big_c[1], 2.9, bx0 - 1, bx1 + 1))
    a = a.union(big)

    # back tab with a hole (YZ plane): flat top, the overhanging back
    # corner rounded down into the plate's back edge
    tx0 = 35.0
    ty0, ty1 = 93.8, 100.0
    t_top = 157.0
    rc = 2.6
    pl = cq.Plane(origin=(tx0, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    tab = (cq.Workplane(pl).moveTo(ty0, A_Z1 - 0.01)
           .lineTo(ty1 - rc, A_Z1 - 0.01)
           .threePointArc((ty1 - rc * (1 - math.cos(math.pi / 4)),
                           A_Z1 + rc * (1 - math.sin(math.pi / 4))),
                          (ty1, A_Z1 + rc))
           .lineTo(ty1, t_top).lineTo(ty0, t_top).close()
           .extrude(A_EAR_T))
    tab = tab.cut(yz_cyl(0.5 * (ty0 + ty1), 153.4, 1.7, tx0 - 1, tx0 + A_EAR_T + 1))
    a = a.union(tab)

    # hollow rib box under the plate, just behind the front edge
    a = a.union(box(UB_X0, UB_X1, UB_Y0, UB_Y1, UB_Z0, A_Z0 + 0.01)
                .cut(box(UB_X0 + 0.9, UB_X1 - 0.9, UB_Y0 + 0.9, UB_Y1 - 0.9,
                         UB_Z0 - 1, A_Z0 - 0.6)))
    a = a.union(box(46.8, 50.8, UB_Y0, UB_Y1, 133.6, UB_Z0 + 0.01))
    # small hollow boss near the back and a locating peg at the back notch
    a = a.union(box(29.0, 37.0, 87.3, 90.5, 135.6, A_Z0 + 0.01)
                .cut(box(29.9, 36.1, 88.2, 89.6, 135.0, A_Z0 - 0.6)))
    a = a.union(box(55.5, 59.5, 92.8, 95.2, 133.6, A_Z0 + 0.01))
    return a


# =================================================================
# Parts B and C : tilt brackets (C is the mirror of B about Y = 41,
# shifted along +X, with a pivot pin instead of the pivot hole)
# =================================================================
BR_MIRROR_Y = 41.0
BR_SHIFT_X = 79.0
# frame (servo cradle), coordinates given for B
FR_X0, FR_X1 = 95.8, 154.4
FR_Y0, FR_Y1 = 15.1, 30.3
FR_Z0, FR_Z1 = 127.2, 143.2
FR_BLOCK_WL = 10.5
FR_BLOCK_WR = 11.5
FR_WALL_Y0 = 26.0
GROOVE_Z = (136.3, 141.7)
GROOVE_DEPTH = 8.7
# web
WEB_Y0, WEB_Y1 = 37.0, 41.0
LUG_C = (160.8, 100.3)
LUG_R = 7.7
LUG_HOLE_R = 4.1
LUG_Y1_B = 44.5                  # B lug is thicker than the web
PIN_R = 3.1
PIN_LEN = 3.0
WEB_TOP = 124.5
TR_Z_WEB = 124.5
TR_Z_BOT = 123.0
WEB_LEFT_Z = 122.3
WEB_BOT_X = 134.2
WEB_FILLET_R = 3.0
WEB_XR = 153.0
CUTOUT = [(118.1, 120.3), (143.0, 120.3), (143.0, 106.2), (134.2, 106.2)]
BLOCK_FILLET = 2.2
BLOCK_FILLET_L = 1.0
LEDGE_Y = 34.0
LEDGE_Z = 132.0
RIB_X = (111.0, 135.2)
RIB_W = 3.4
STRAP_X = 141.5
STRAP_R = 5.2
STRAP_GAP = 0.6


def web_outline(y0, y1):
    """bracket web (XZ plane): straight right edge, concave fillet onto the
    flat top of the pivot lug, round lug end, straight bottom, sloped left"""
    cx, cz = LUG_C
    xr = WEB_XR                           # right edge of the web
    xl = FR_X0 + 1.3                      # left edge at the top
    rf = WEB_FILLET_R
    ztop = cz + LUG_R
    a45 = math.sqrt(0.5)
    pl = cq.Plane(origin=(0, y1, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    w = (cq.Workplane(pl).moveTo(xl, WEB_TOP)
         .lineTo(xr, WEB_TOP)
         .lineTo(xr, ztop + rf)
         .threePointArc((xr + rf * (1 - a45), ztop + rf * (1 - a45)), (xr + rf, ztop))
         .lineTo(cx, ztop)
         .threePointArc((cx + LUG_R, cz), (cx, cz - LUG_R))
         .lineTo(WEB_BOT_X, cz - LUG_R)
         .lineTo(xl, WEB_LEFT_Z)
         .close()
         .extrude(y1 - y0))
    return w


def strap_shape(d, y0, y1):
    cx, cz = LUG_C
    pts = [(STRAP_X, cz - LUG_R + d), (cx, cz - LUG_R + d),
           (cx, cz + LUG_R - d), (STRAP_X, cz - LUG_R + 2 * STRAP_R - d)]
    st = xz_prism(pts, y0, y1)
    st = st.union(xz_cyl(cx, cz, LUG_R - d, y0, y1))
    st = st.union(xz_cyl(STRAP_X, cz - LUG_R + STRAP_R, STRAP_R - d, y0, y1))
    return st


def make_bracket(with_hole):
    fx0, fx1 = FR_X0, FR_X1
    # cradle: one block, rounded along the outer top edges, with the
    # servo pocket (U) and the inward facing grooves for the servo ears
    fr = box(fx0, fx1, FR_Y0, FR_Y1, FR_Z0, FR_Z1)
    # small round on the outer top edge of the left block
    fr = (fr.edges(cq.selectors.BoxSelector((fx0 - 0.1, FR_Y0 - 1, FR_Z1 - 0.1),
                                            (fx0 + 0.1, FR_Y1 + 1, FR_Z1 + 0.1)))
          .fillet(BLOCK_FILLET_L))
    # larger rounds on the right block top edge and along the wall side
    fr = (fr.edges(cq.selectors.BoxSelector((fx1 - 0.1, FR_Y0 - 1, FR_Z1 - 0.1),
                                            (fx1 + 0.1, FR_Y1 + 1, FR_Z1 + 0.1))
                   + cq.selectors.BoxSelector((fx0 - 1, FR_Y1 - 0.1, FR_Z1 - 0.1),
                                              (fx1 + 1, FR_Y1 + 0.1, FR_Z1 + 0.1))
                   + cq.selectors.BoxSelector((fx0 - 0.1, FR_Y1 - 0.1, FR_Z0 - 0.1),
                                              (fx0 + 0.1, FR_Y1 + 0.1, FR_Z1 - 0.5))
                   + cq.selectors.BoxSelector((fx1 - 0.1, FR_Y1 - 0.1, FR_Z0 - 0.1),
                                              (fx1 + 0.1, FR_Y1 + 0.1, FR_Z1 - 0.5)))
          .fillet(BLOCK_FILLET))
    fr = fr.cut(box(fx0 + FR_BLOCK_WL, fx1 - FR_BLOCK_WR, FR_Y0 - 1, FR_WALL_Y0,
                    FR_Z0 - 1, FR_Z1 + 1))
    fr = fr.cut(box(fx0 + FR_BLOCK_WL - GROOVE_DEPTH, fx0 + FR_BLOCK_WL + 1,
                    FR_Y0 - 1, FR_WALL_Y0, GROOVE_Z[0], GROOVE_Z[1]))
    fr = fr.cut(box(fx1 - FR_BLOCK_WR - 1, fx1 - FR_BLOCK_WR + GROOVE_DEPTH,
                    FR_Y0 - 1, FR_WALL_Y0, GROOVE_Z[0], GROOVE_Z[1]))
    br = fr

    # sloped transition from the cradle down to the web, with a narrow ledge
    trans = yz_prism([(FR_Y1 - 0.01, LEDGE_Z), (LEDGE_Y, LEDGE_Z),
                      (WEB_Y1, TR_Z_WEB), (WEB_Y1, TR_Z_WEB - 4.5),
                      (WEB_Y0, TR_Z_WEB - 4.5), (WEB_Y0, TR_Z_BOT),
                      (FR_Y1 - 0.01, FR_Z0 + 2.6)],
                     fx0 + 1.3, WEB_XR)
    br = br.union(trans)
    # two small ribs continuing the slope up to the cradle wall
    slope = (LEDGE_Z - TR_Z_WEB) / (WEB_Y1 - LEDGE_Y)
    rib_top = LEDGE_Z + slope * (LEDGE_Y - FR_Y1)
    for nx in RIB_X:
        br = br.union(yz_prism([(FR_Y1 - 0.01, LEDGE_Z - 0.01),
                                (LEDGE_Y, LEDGE_Z - 0.01),
                                (FR_Y1 - 0.01, rib_top)],
                               nx, nx + RIB_W))

    # web in the XZ plane
    web = web_outline(WEB_Y0, WEB_Y1)
    # triangular lightening cut-out
    web = web.cut(xz_prism(CUTOUT, WEB_Y0 - 1, WEB_Y1 + 1))
    br = br.union(web)

    if with_hole:
        # second layer (link strap) behind the lug, joined to the web by a
        # slightly smaller neck so a shallow groove runs round the lug rim
        cx, cz = LUG_C
        strap = strap_shape(0.0, WEB_Y1 + STRAP_GAP, LUG_Y1_B)
        strap = strap.union(strap_shape(0.7, WEB_Y1 - 0.01, WEB_Y1 + STRAP_GAP + 0.01))
        br = br.union(strap)
        br = br.cut(xz_cyl(cx, cz, LUG_HOLE_R, WEB_Y0 - 1, LUG_Y1_B + 1))
    else:
        # pivot pin protruding from the outer web face
        br = br.union(xz_cyl(LUG_C[0], LUG_C[1], PIN_R,
                             WEB_Y1 - 0.01, WEB_Y1 + PIN_LEN))
    return br


def make_B():
    return make_bracket(True)


def make_C():
    c = make_bracket(False)
    c = c.mirror("XZ", basePointVector=(0, BR_MIRROR_Y, 0))
    return c.translate((BR_SHIFT_X, 0, 0))


partA = make_A()
partB = make_B()
partC = make_C()
partD = make_D()
partE = make_E()
partF = make_F()

result = (partA.union(partB).union(partC)
          .union(partD).union(partE).union(partF))
